import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
U = 19.05            # key pitch
MARGIN = 12.0        # outermost key centre -> plate edge
T = 5.2              # plate thickness
HOLE = 14.0          # switch cut-out (square)
HOLE_R = 0.5         # switch cut-out corner radius
POCKET = 17.5        # shallow underside relief around each switch cut-out
POCKET_D = 0.3       # depth of that relief
POCKET_R = 2.0       # relief corner radius
N_SIDE = 6           # key columns per half
N_ROWS = 4           # full-width rows

# bottom (thumb) row
THUMB_1U = [2.5, 3.5, 4.5]   # 1u key centres (in units from the middle)
THUMB_2U = 1.0               # 2u key centre (units from the middle)
STAB_DX = 11.9               # stabiliser offset from 2u key centre
STAB_W = 6.75
STAB_TOP = 5.5               # stab cut-out top above key centre
STAB_BOT = 8.1               # stab cut-out bottom below key centre

# central split slot
NECK_W = 13.3                # narrow mouth at the back edge (part of outline)
SLOT_W = 20.3                # wide part of the slot (cut after rounding)
NECK_L = 16.6                # length of the narrow mouth from the back edge
SLOT_END = 3 * U + 11.5      # depth of the slot end below row-0 centre
SLOT_TOP_R = 1.2             # concave radius where the slot widens
LIP_R = 1.5                  # convex radius on the lip where the slot widens

# edge treatment
R_CORNER = 2.2               # vertical outer corner radius
R_INNER = 1.5                # concave notch corner radius
R_MOUTH = 2.2                # slot mouth corner radius
R_TOP = 2.0                  # top edge round-over of the outline

# ---------------- derived ----------------
W = N_SIDE * U + MARGIN                  # half width of main block
Y_TOP = MARGIN                           # back edge (row 0 at y = 0)
Y_MAIN_BOT = -(N_ROWS - 1) * U - MARGIN  # front edge of main block
Y_THUMB = -N_ROWS * U                    # thumb-row centre
Y_BOT = Y_THUMB - MARGIN                 # front edge of thumb strip
BW = THUMB_1U[-1] * U + MARGIN           # half width of thumb strip
Y_NECK = Y_TOP - NECK_L                  # where the slot widens
Y_END = -SLOT_END                        # lowest point of the slot
NW = NECK_W / 2
Y_NECK_BOT = Y_NECK - 3.0                # neck notch runs into the wide slot

# ---------------- outline (with the narrow neck notch) ----------------
pts = [
    (-W, Y_TOP), (-W, Y_MAIN_BOT), (-BW, Y_MAIN_BOT), (-BW, Y_BOT),
    (BW, Y_BOT), (BW, Y_MAIN_BOT), (W, Y_MAIN_BOT), (W, Y_TOP),
    (NW, Y_TOP), (NW, Y_NECK_BOT), (-NW, Y_NECK_BOT), (-NW, Y_TOP),
]
plate = cq.Workplane("XY").polyline(pts).close().extrude(T)


def _near(pts_xy, tol=1e-3):
    def f(e):
        c = e.Center()
        return any(abs(c.x - x) < tol and abs(c.y - y) < tol for x, y in pts_xy)
    return f


outer_xy = [(-W, Y_TOP), (-W, Y_MAIN_BOT), (-BW, Y_BOT), (BW, Y_BOT),
            (W, Y_MAIN_BOT), (W, Y_TOP)]
inner_xy = [(-BW, Y_MAIN_BOT), (BW, Y_MAIN_BOT)]
mouth_xy = [(-NW, Y_TOP), (NW, Y_TOP)]

plate = plate.edges("|Z").filter(_near(outer_xy)).fillet(R_CORNER)
plate = plate.edges("|Z").filter(_near(inner_xy)).fillet(R_INNER)
plate = plate.edges("|Z").filter(_near(mouth_xy)).fillet(R_MOUTH)

# round over the whole top outline (neck walls included)
plate = plate.faces(">Z").edges().fillet(R_TOP)

# ---------------- wide split slot, cut with sharp edges ----------------
y_c = Y_END + SLOT_W / 2                 # centre of the round end
stub_top = Y_NECK + 3.0                  # short neck stub to shape the lip corner
slot_rect = (cq.Workplane("XY").workplane(offset=-1)
             .center(0, (Y_NECK + y_c) / 2)
             .rect(SLOT_W, Y_NECK - y_c).extrude(T + 2)
             .edges("|Z").edges(">Y").fillet(SLOT_TOP_R))
stub = (cq.Workplane("XY").workplane(offset=-1)
        .center(0, (Y_NECK - 1 + stub_top) / 2)
        .rect(NECK_W, stub_top - Y_NECK + 1).extrude(T + 2))
slot_end = (cq.Workplane("XY").workplane(offset=-1).center(0, y_c)
            .circle(SLOT_W / 2).extrude(T + 2))
slot_tool = slot_rect.union(stub).union(slot_end)
# concave tool corners at the step -> rounded convex lip corners on the plate
lip_xy = [(-NW, Y_NECK), (NW, Y_NECK)]
slot_tool = slot_tool.edges("|Z").filter(_near(lip_xy)).fillet(LIP_R)
plate = plate.cut(slot_tool)

# ---------------- switch cut-outs ----------------
key_pts = []
for r in range(N_ROWS):
    for i in range(1, N_SIDE + 1):
        for s in (-1, 1):
            key_pts.append((s * i * U, -r * U))
for c in THUMB_1U:
    for s in (-1, 1):
        key_pts.append((s * c * U, Y_THUMB))
for s in (-1, 1):
    key_pts.append((s * THUMB_2U * U, Y_THUMB))

holes = (cq.Workplane("XY").workplane(offset=-1).pushPoints(key_pts)
         .rect(HOLE, HOLE).extrude(T + 2).edges("|Z").fillet(HOLE_R))
plate = plate.cut(holes)

# stabiliser cut-outs for the two 2u keys
stab_pts = []
stab_h = STAB_TOP + STAB_BOT
stab_cy = Y_THUMB + (STAB_TOP - STAB_BOT) / 2
for s in (-1, 1):
    for d in (-1, 1):
        stab_pts.append((s * THUMB_2U * U + d * STAB_DX, stab_cy))
stabs = (cq.Workplane("XY").workplane(offset=-1).pushPoints(stab_pts)
         .rect(STAB_W, stab_h).extrude(T + 2).edges("|Z").fillet(HOLE_R))
plate = plate.cut(stabs)

# shallow relief pockets on the underside around every switch
if POCKET_D > 0:
    pockets = (cq.Workplane("XY").workplane(offset=-1).pushPoints(key_pts)
               .rect(POCKET, POCKET).extrude(POCKET_D + 1)
               .edges("|Z").fillet(POCKET_R))
    plate = plate.cut(pockets)

result = plate

VIEW = {"azimuth": 45, "elevation": 26}
